import cadquery as cq
import math

# ---------------------------------------------------------------
# Two-piece cross clamp: two identical clamping halves whose bores
# cross at 90 deg; the whole part is rotated 45 deg about Y.
# All driving dimensions in "units" (1 unit = 0.2 mm).
# ---------------------------------------------------------------
U = 0.2

L = 482          # half length along its bore
W = 237          # half width
Y0, Y1 = -250, 62   # front / back face of a half (local y)
CC = 23.5        # chamfer on the long corner edges
FC = 24          # chamfer around front / back faces
CF1, CF2 = 31, 45  # corner facets: inset on front/back face, depth along the corner chamfer
BORE_D = 131     # tube bore
BORE_Y = -90     # bore axis position (local y)
BORE_CH = 5      # bore edge chamfer
SLOT_W = 8      # clamping slot width
SLOT_CH = 5      # chamfer on slot edges at the back face
SLOT_S = 148     # slot inner end (slot only at +s end)

EAR_C = 128.7    # ear centre (local s = t)
EAR_A = 53       # ear half size (octagon apothem)
EAR_CH = 31      # ear corner chamfer
EAR_Y0, EAR_Y1 = -184, -12
EAR_HOLE = 25
EAR_CSK = 40     # countersink diameter
EAR_BCH = 5

NOTCH_S, NOTCH_T, NOTCH_CH = 76, 72, 29   # front notch under the ear

CS_S = 186       # clamp screw positions (+/- along s)
CS_Y = 6.5
CS_HOLE, CS_CB, CS_CB_D = 22, 54, 25
NUT_AF, NUT_D = 45, 22

CTR_HOLE, CTR_CSK, CTR_DEPTH = 26, 40, 60

WALL_IN, WALL_OUT, WALL_H = 121, 146, 25  # ribs on back face
POCK_W, POCK_S0, POCK_S1, POCK_D = 12, 150, 222, 12  # blind pocket at -s end


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def prism_st(pts, y0, y1):
    """polygon in local (s,t) plane extruded along local y"""
    # workplane XZ: local x = s, local y(plane) = t ; normal = -Y
    wp = cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close()
    return wp.extrude(y1 - y0)


def cyl(p, d, r, h):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, h, cq.Vector(*p), cq.Vector(*d)))


def csk(p, d_hole, d_csk):
    """45 deg countersink cone at point p on a -Y facing face"""
    h = (d_csk - d_hole) / 2
    cone = cq.Solid.makeCone(d_csk / 2 + 1, d_hole / 2, h + 1,
                             cq.Vector(p[0], p[1] - 1, p[2]), cq.Vector(0, 1, 0))
    return cq.Workplane("XY").add(cone)


def bore_cutter(seam_side):
    """tube bore with 45 deg edge chamfers, revolved so that the surface seam
    lies on a side that is hidden in the standard views"""
    R = BORE_D / 2
    prof = [(-L / 2 - 2, 0), (-L / 2 - 2, R + BORE_CH + 2), (-L / 2 + BORE_CH, R),
            (L / 2 - BORE_CH, R), (L / 2 + 2, R + BORE_CH + 2), (L / 2 + 2, 0)]
    nrm = (0, 0, -1) if seam_side == "-y" else (0, -1, 0)   # seam at -y or at +t
    bpl = cq.Plane(origin=(0, BORE_Y, 0), xDir=(1, 0, 0), normal=nrm)
    return cq.Workplane(bpl).polyline(prof).close().revolve(360, (0, 0, 0), (1, 0, 0))


def ear_hole_cutter():
    return cyl((EAR_C, EAR_Y0 - 1, EAR_C), (0, 1, 0), EAR_HOLE / 2, 400)


def half(center_hole, seam_side):
    # main bar: local x = s, local z = t, local y = y
    b = box(-L / 2, L / 2, Y0, Y1, -W / 2, W / 2)
    b = b.edges("|Y").chamfer(CC)
    b = b.faces("<Y or >Y").edges().chamfer(FC * 0.99)
    # deeper corner facets where the long corner chamfers meet front / back faces
    for ss in (1, -1):
        for st in (1, -1):
            ncc = cq.Vector(ss, 0, st).normalized()
            e = cq.Vector(-st, 0, ss).normalized()
            dcc = (L / 2 + W / 2 - CC) / math.sqrt(2)
            pl = cq.Plane(origin=(0, 0, 0), xDir=ncc, normal=e)
            for yf, sg in ((Y0, -1), (Y1, 1)):
                tri = [(dcc - 3 * CF1, yf + sg * 2 * CF2), (dcc + 2 * CF1, yf - sg * 3 * CF2),
                       (dcc + 150, yf + sg * 150)]
                w = cq.Workplane(pl).polyline(tri).close().extrude(300, both=True)
                b = b.cut(w)

    # front notch below the ear
    n = prism_st([(NOTCH_S, NOTCH_T + NOTCH_CH), (NOTCH_S, 400), (400, 400),
                  (400, NOTCH_T), (NOTCH_S + NOTCH_CH, NOTCH_T)], Y0 - 1, EAR_Y0)
    b = b.cut(n)

    # ear (octagonal prism) with through hole
    e0, e1 = EAR_C - EAR_A, EAR_C + EAR_A
    ear = box(e0, e1, EAR_Y0, EAR_Y1, e0, e1).edges("|Y").chamfer(EAR_CH)
    ear = ear.faces("<Y").edges().chamfer(3)
    ear = ear.faces(">Y").edges().chamfer(EAR_BCH)
    b = b.union(ear)
    b = b.cut(ear_hole_cutter())
    b = b.cut(csk((EAR_C, EAR_Y0, EAR_C), EAR_HOLE, EAR_CSK))

    # bore with 45 deg edge chamfers
    b = b.cut(bore_cutter(seam_side))

    # clamping slot from bore to back face, only at the +s end, V-shaped tip
    hw = SLOT_W / 2
    slot = prism_st([(SLOT_S, 0), (SLOT_S + hw, hw), (L, hw), (L, -hw), (SLOT_S + hw, -hw)],
                    BORE_Y, Y1 + 1)
    b = b.cut(slot)
    def mouth(e):
        p0, p1 = e.startPoint(), e.endPoint()
        if e.geomType() != "LINE":
            return False
        ok = True
        for p in (p0, p1):
            on_t = abs(p.z) <= hw + 0.5 and p.x >= SLOT_S - 1
            on_back = p.y >= Y1 - 0.5
            on_end = p.x >= L / 2 - FC - 0.5 and p.y >= BORE_Y + BORE_D / 2 + 0.5
            ok = ok and on_t and (on_back or on_end)
        return ok
    sel = [e for e in b.edges().vals() if mouth(e)]
    try:
        b = b.newObject(sel).chamfer(SLOT_CH)
    except Exception:
        pass

    # blind oblong pocket on the back face at the -s end
    pk = (cq.Workplane("XZ", origin=(0, Y1 + 1, 0))
          .center(-(POCK_S0 + POCK_S1) / 2, 0)
          .slot2D(POCK_S1 - POCK_S0, POCK_W, 0).extrude(POCK_D + 1))
    b = b.cut(pk)

    # clamp screws (along t): counterbore on -t face, hex nut pocket on +t face
    for s in (CS_S, -CS_S):
        b = b.cut(cyl((s, CS_Y, -W), (0, 0, 1), CS_HOLE / 2, 2 * W))
        b = b.cut(cyl((s, CS_Y, -W / 2 - 1), (0, 0, 1), CS_CB / 2, CS_CB_D + 1))
        nut = (cq.Workplane(cq.Plane(origin=(s, CS_Y, W / 2 + 1), xDir=(1, 0, 0), normal=(0, 0, 1)))
               .polygon(6, NUT_AF / math.cos(math.pi / 6))
               .extrude(-(NUT_D + 1)))
        b = b.cut(nut)

    # centre screw hole
    if center_hole:
        b = b.cut(cyl((0, Y0 - 1, 0), (0, 1, 0), CTR_HOLE / 2, CTR_DEPTH + 1))
        b = b.cut(csk((0, Y0, 0), CTR_HOLE, CTR_CSK))

    # locating ribs on back face
    for sgn, (t0, t1) in ((1, (-66, 78)), (-1, (-78, 66))):
        pts = [(sgn * WALL_IN, Y1 - 1), (sgn * WALL_IN, Y1 + WALL_H),
               (sgn * WALL_OUT, Y1 - 1)]
        rib = (cq.Workplane("XY", origin=(0, 0, t0)).polyline(pts).close()
               .extrude(t1 - t0))
        b = b.union(rib)
    return b


def place_a(w):
    return w.rotate((0, 0, 0), (0, 1, 0), -45)


def place_b(w):
    return w.rotate((0, 0, 0), (0, 1, 0), -45).rotate((0, 0, 0), (0, 0, 1), 180)


A = place_a(half(True, "-y"))
B = place_b(half(False, "+t"))
part = A.union(B)
# keep both tube bores and the ear holes clear where the halves overlap
for place, seam in ((place_a, "-y"), (place_b, "+t")):
    part = part.cut(place(bore_cutter(seam))).cut(place(ear_hole_cutter()))
result = cq.Workplane("XY").add(part.val().scale(U))
